import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
D = 50.0                 # OD of the vertical down-pipe
T = 0.12 * D             # rim left round the socket recess at the pipe foot
PIPE_LEN = 5.34 * D      # straight vertical pipe (bottom -> joint with fitting)
RECESS_DEPTH = 0.10 * D  # shallow socket recess in the bottom end of the pipe
RECESS_CH = 0.03 * D     # chamfer on the recess mouth

D2 = 0.985 * D           # OD of the offset fitting (ball-jointed bend)
Z_BEND = 5.78 * D        # height of the bend point on the pipe axis
SLOPE = 20.0             # sloped leg angle above horizontal (deg)
JOINT_R = 0.03 * D       # round on the fitting's lower edge at the joint

BOX_X0 = 1.47 * D        # outlet box, start in X
BOX_X1 = 3.63 * D        # outlet box, end in X
BOX_W = 1.00 * D         # outlet box width (Y)
BOX_R = 0.41 * D         # plan corner radius of the box
BOX_TOP = 8.10 * D       # top rim height
BOX_BOT = 6.50 * D       # underside of the box
BOX_BOT_R = 0.40 * D     # round-over of the box bottom edges

IN_L = 1.76 * D          # opening length
IN_W = 0.71 * D          # opening width
IN_R = 0.15 * D          # opening corner radius
POCKET_DEPTH = 0.70 * D  # depth of the outlet pocket
POCKET_R = 0.05 * D      # round at the pocket floor

# ---------------- derived ----------------
ta = math.tan(math.radians(SLOPE))
r2 = D2 / 2
box_len = BOX_X1 - BOX_X0
box_cx = 0.5 * (BOX_X0 + BOX_X1)
X_END = BOX_X1 - r2              # end of the sloped leg (inside the box)


def axis_z(x):
    return Z_BEND + x * ta


def ball_jointed_tube(radius, z_start, x_end):
    """vertical run + ball joint + sloped run, all of one radius"""
    up = cq.Solid.makeCylinder(radius, Z_BEND - z_start,
                               cq.Vector(0, 0, z_start), cq.Vector(0, 0, 1))
    # keep the cylinder seam on the back (+Y) side
    up = up.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), 90)
    joint = cq.Solid.makeSphere(radius, cq.Vector(0, 0, Z_BEND),
                                angleDegrees1=-90, angleDegrees2=90)
    run = cq.Vector(x_end, 0, axis_z(x_end) - Z_BEND)
    leg = cq.Solid.makeCylinder(radius, run.Length,
                                cq.Vector(0, 0, 0), cq.Vector(0, 0, 1))
    leg = (leg.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), 90)
              .rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), 90 - SLOPE)
              .translate(cq.Vector(0, 0, Z_BEND)))
    return cq.Workplane("XY").add(up.fuse(joint).fuse(leg).clean())


# ---------------- vertical pipe ----------------
pipe = (cq.Workplane("XY")
        .circle(D / 2)
        .extrude(PIPE_LEN)
        .rotate((0, 0, 0), (0, 0, 1), 90))
recess = (cq.Workplane("XY").workplane(offset=-1.0)
          .circle(D / 2 - T).extrude(RECESS_DEPTH + 1.0))
pipe = pipe.cut(recess)
pipe = (pipe.faces("<Z").edges(cq.selectors.RadiusNthSelector(0))
        .chamfer(RECESS_CH))

# ---------------- fitting: ball-jointed offset leg ----------------
leg = ball_jointed_tube(r2, PIPE_LEN, X_END)

# ---------------- outlet box ----------------
box = (cq.Workplane("XY").workplane(offset=BOX_BOT)
       .center(box_cx, 0)
       .sketch().rect(box_len, BOX_W).vertices().fillet(BOX_R).finalize()
       .extrude(BOX_TOP - BOX_BOT))
box = box.faces("<Z").edges().fillet(BOX_BOT_R)

outer = leg.union(box)
# the fitting starts at the joint with the pipe
below_joint = (cq.Workplane("XY").workplane(offset=PIPE_LEN - 3 * D)
               .rect(4 * D, 4 * D).extrude(3 * D))
outer = outer.cut(below_joint)
# small round on the lower edge of the fitting where it meets the pipe
outer = outer.faces("<Z").edges().fillet(JOINT_R)

# ---------------- outlet opening (blind pocket) ----------------
pocket = (cq.Workplane("XY").workplane(offset=BOX_TOP - POCKET_DEPTH)
          .center(box_cx, 0)
          .sketch().rect(IN_L, IN_W).vertices().fillet(IN_R).finalize()
          .extrude(POCKET_DEPTH + 1.0)
          .faces("<Z").edges().fillet(POCKET_R))

fitting = outer.cut(pocket)

result = pipe.union(fitting)

VIEW = {"azimuth": 45, "elevation": 26}
